"""Octagonal stamp / tile with the character 漢 engraved in its top face.

Plate : regular octagon (vertex on +X), flat top and bottom.
Glyph : bold gothic-style 漢 cut as a flat-bottomed pocket, rotated about Z.
All glyph coordinates are given in a local text frame (u right, v up, mm for a
50 mm circumradius plate) and scale with the plate.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm / deg) ----------------
R_OCT = 50.0            # octagon circumradius (a vertex lies on +X)
THICK = 16.4            # plate thickness
DEPTH = 9.0             # engraving depth of the character
TEXT_ROT = 25.0         # rotation of the character about Z (CCW seen from top)
GLYPH_SCALE = R_OCT / 50.0   # glyph drawn for a 50 mm plate, scaled with it
GLYPH_DX, GLYPH_DY = 0.0, 0.0  # glyph centre offset on the plate

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- octagonal plate ----------------
plate = (
    cq.Workplane("XY")
    .polygon(8, 2 * R_OCT)
    .extrude(THICK)
    .translate((0, 0, -THICK / 2))
)
Z_TOP = THICK / 2
Z_FLOOR = Z_TOP - DEPTH
OVERCUT = 1.0           # tool runs out above the top face


def _p(pt):
    return (pt[0] * GLYPH_SCALE, pt[1] * GLYPH_SCALE)


def prism_poly(pts):
    """Straight-sided stroke: closed polygon in the text frame."""
    return (
        cq.Workplane("XY")
        .workplane(offset=Z_FLOOR)
        .polyline([_p(p) for p in pts])
        .close()
        .extrude(DEPTH + OVERCUT)
    )


def prism_rect(u0, u1, v0, v1):
    return prism_poly([(u0, v0), (u1, v0), (u1, v1), (u0, v1)])


def prism_path(start, segs):
    """Stroke outline of lines and arcs: ('L', end) or ('A', mid, end)."""
    wp = cq.Workplane("XY").workplane(offset=Z_FLOOR).moveTo(*_p(start))
    for s in segs:
        if s[0] == "L":
            wp = wp.lineTo(*_p(s[1]))
        else:
            wp = wp.threePointArc(_p(s[1]), _p(s[2]))
    return wp.close().extrude(DEPTH + OVERCUT)


strokes = []

# ---- left radical: two dots and the rising stroke ----
strokes.append(prism_poly([(-21.7, 26.9), (-12.3, 20.0), (-15.4, 15.8), (-25.4, 23.7)]))
strokes.append(prism_poly([(-24.5, 12.1), (-15.4, 6.0), (-18.8, 1.7), (-27.6, 8.8)]))
strokes.append(
    prism_path(
        (-18.9, -3.1),
        [
            ("L", (-14.8, -5.8)),
            ("A", (-17.8, -16.0), (-23.1, -28.1)),
            ("L", (-28.0, -24.4)),
            ("A", (-22.6, -12.0), (-18.9, -3.1)),
        ],
    )
)

# ---- top component: long bar crossed by two verticals, closed below ----
BAR_V = (20.5, 25.0)
strokes.append(prism_rect(-11.6, 27.4, *BAR_V))        # long top bar
strokes.append(prism_rect(-4.3, 0.3, 13.8, 27.6))      # left vertical (pokes above bar)
strokes.append(prism_rect(15.1, 19.8, 14.0, 27.7))     # right vertical (pokes above bar)
strokes.append(prism_rect(-4.3, 19.8, 13.8, 17.8))     # lower closing bar

# ---- central vertical: from the top component down to the sweeps ----
strokes.append(
    prism_poly(
        [(5.1, 14.0), (10.15, 14.0), (10.15, -6.5), (9.0, -6.5),
         (9.0, -16.2), (4.2, -16.2), (4.2, -6.5), (5.1, -6.5)]
    )
)

# ---- box (split in two counters by the central vertical) ----
BOX_U = (-8.9, 24.6)
BOX_V = (-1.2, 10.8)
BOX_W = 4.6
strokes.append(prism_rect(BOX_U[0], BOX_U[1], 6.6, BOX_V[1]))          # top
strokes.append(prism_rect(BOX_U[0], BOX_U[1], BOX_V[0], 2.7))          # bottom
strokes.append(prism_rect(BOX_U[0], BOX_U[0] + BOX_W, *BOX_V))         # left
strokes.append(prism_rect(BOX_U[1] - 4.9, BOX_U[1], *BOX_V))           # right

# ---- two horizontals of the lower part ----
strokes.append(prism_rect(-9.3, 24.8, -8.5, -4.4))
strokes.append(prism_rect(-12.5, 27.5, -16.0, -11.7))

# ---- left-falling sweep ----
strokes.append(
    prism_path(
        (1.6, -15.5),
        [
            ("L", (7.6, -16.0)),
            ("A", (3.3, -21.4), (-8.8, -27.7)),
            ("L", (-10.8, -27.7)),
            ("L", (-13.0, -23.2)),
            ("A", (-4.8, -20.9), (1.6, -16.0)),
        ],
    )
)

# ---- right-falling sweep ----
strokes.append(
    prism_path(
        (7.6, -15.5),
        [
            ("L", (13.6, -16.0)),
            ("A", (19.1, -19.9), (28.6, -22.6)),
            ("L", (26.3, -28.0)),
            ("A", (14.5, -22.8), (7.6, -16.0)),
        ],
    )
)

# ---------------- engrave ----------------
pocket = strokes[0]
for s in strokes[1:]:
    pocket = pocket.union(s)
pocket = pocket.rotate((0, 0, 0), (0, 0, 1), TEXT_ROT).translate((GLYPH_DX, GLYPH_DY, 0))

result = plate.cut(pocket)
